import cadquery as cq

# Driving dimensions (mm) -- round cap / puck with rounded top and bottom rims
DIAMETER = 40.0        # outer diameter
HEIGHT = 9.8           # overall thickness
TOP_FILLET = 2.7       # rounding of the upper rim
BOTTOM_FILLET = 3.8    # rounding of the lower rim (slightly larger)

VIEW = {"azimuth": 45, "elevation": 26}

R = DIAMETER / 2.0

# Half cross-section in the XZ plane, revolved about the Z axis
profile = (
    cq.Workplane("XZ")
    .moveTo(0, 0)
    .lineTo(R - BOTTOM_FILLET, 0)
    .radiusArc((R, BOTTOM_FILLET), -BOTTOM_FILLET)
    .lineTo(R, HEIGHT - TOP_FILLET)
    .radiusArc((R - TOP_FILLET, HEIGHT), -TOP_FILLET)
    .lineTo(0, HEIGHT)
    .close()
)
result = profile.revolve(360, (0, 0, 0), (0, 1, 0))
